import math
import cadquery as cq

# ---------------------------------------------------------------
# Twin-engine wide-body airliner (787-like), nose pointing +Z,
# wings spanning X, fin pointing +Y (belly / engines on -Y side).
# Units: mm (about 1/265 of the real aircraft)
# ---------------------------------------------------------------

# fuselage: constant section between Z_TAIL and Z_NOSE, lofted nose and tail
R_FUS = 10.8
Z_TAIL, Z_NOSE = -40.0, 80.0
NOSE_STATIONS = [          # (z, y-centre, half-width, half-height)
    (Z_NOSE, 0.0, R_FUS, R_FUS),
    (88.0, -0.1, 10.2, 10.55),
    (97.0, -0.4, 9.5, 10.0),
    (105.0, -1.45, 7.95, 8.5),
    (112.0, -3.6, 4.95, 5.5),
    (116.8, -4.8, 2.1, 2.4),
    (118.6, -5.0, 0.35, 0.4),
]
TAIL_STATIONS = [
    (Z_TAIL, 0.0, R_FUS),
    (-56.0, 0.8, 9.85),
    (-70.0, 1.9, 8.7),
    (-88.0, 4.2, 6.0),
    (-106.0, 6.3, 3.4),
    (-113.8, 6.8, 1.1),
]

# belly (wing-body) fairing stations: (z, y-centre, half-width, half-height)
FAIRING_STATIONS = [
    (50.0, -6.6, 4.0, 2.0),
    (44.0, -7.0, 9.8, 4.4),
    (33.0, -7.6, 11.2, 4.7),
    (8.0, -8.0, 11.8, 4.35),
    (-15.0, -8.0, 12.1, 4.3),
    (-26.0, -7.6, 10.8, 3.7),
    (-32.0, -7.0, 5.0, 1.5),
]

# main wing  (s = distance from the centre line, z along the fuselage)
S_SIDE = 10.9                   # fuselage side
LE_ROOT_Z = 39.6                # leading edge z at the fuselage side
KINK_S = 38.0                   # planform kink (at the engine)
LE_KINK_Z = 19.6
LE_SLOPE = 0.682                # outboard leading-edge sweep dz/ds
TE_ROOT_Z, TE_KINK_Z = -8.0, -9.4
TE_SLOPE = 0.405                # outboard trailing-edge sweep dz/ds
WING_Y_ROOT = -5.7              # mean line height at the fuselage side
DIHEDRAL = 0.11                 # dY/ds
S_OUT = 104.0                   # start of the up-turned raked tip
T_ROOT, T_KINK, T_OUT = 0.115, 0.10, 0.09
# raked, up-turned wing tip sections: (s, le z, te z, y, cant deg)
TIP_SECTIONS = [
    (110.1, -29.6, -38.6, 6.3, 12.0),
    (113.6, -35.0, -42.0, 8.7, 45.0),
    (114.3, -42.8, -46.0, 13.6, 80.0),
]

# engines
ENG_X, ENG_Y = 37.7, -10.3
NAC_FRONT, NAC_REAR = 41.2, 19.3
NAC_R = 7.0                     # max nacelle radius
NAC_LIP_R = 6.25
NAC_INLET_R = 5.55
NAC_REAR_R = 5.3
INLET_DEPTH = 4.6               # depth of the fan face behind the lip
SPINNER_R, SPINNER_TIP_DEPTH = 2.6, 0.9

# horizontal tail sections (s, le z, te z, y); last two round off the tip
HT_SECTIONS = [
    (0.0, -82.1, -106.4, 4.5),
    (31.5, -108.6, -116.5, 6.6),
    (33.9, -111.3, -117.3, 6.75),
    (34.8, -114.0, -117.6, 6.8),
]

# vertical fin sections (y, le z, te z); last two round off the tip
VT_SECTIONS = [
    (6.0, -71.3, -102.3),
    (38.5, -103.8, -116.3),
    (40.6, -107.3, -117.2),
    (41.3, -110.0, -117.6),
]
VT_T_ROOT, VT_T_TIP = 0.05, 0.08

# small blade antennas on the crown (+1) and belly (-1): (z, side, y of skin)
ANTENNAS = [(61.5, -1, -R_FUS), (-35.0, -1, -R_FUS),
            (54.5, 1, R_FUS), (-30.5, 1, R_FUS), (-65.7, 1, 10.4)]
ANT_H, ANT_L, ANT_T = 1.2, 1.6, 0.4

# flap track fairings (s, z_front, z_rear)
FLAP_TRACKS = [(27.8, 5.6, -12.7), (45.3, 2.2, -16.5), (61.2, -8.8, -22.3)]
FT_SIZE = 1.25
FT_DROOP = 4.0


# ---------------------------------------------------------------
def naca_half(x, t):
    return 5 * t * (0.2969 * math.sqrt(x) - 0.1260 * x - 0.3516 * x ** 2
                    + 0.2843 * x ** 3 - 0.1015 * x ** 4)


XS = [1.0, 0.7, 0.45, 0.25, 0.1, 0.03, 0.0]


def airfoil_wire(to3d, t):
    """Closed airfoil wire (one spline round the nose + trailing-edge line);
    to3d(u, v) maps chord fraction u and thickness coordinate v (in chord
    units) into a 3D Vector."""
    pts = ([to3d(x, naca_half(x, t)) for x in XS]
           + [to3d(x, -naca_half(x, t)) for x in XS[-2::-1]])
    sp = cq.Edge.makeSpline(pts)
    ln = cq.Edge.makeLine(pts[-1], pts[0])
    return cq.Wire.assembleEdges([sp, ln])


def wing_section(s, z_le, z_te, y_c, t, cant=0.0, side=-1):
    """Airfoil section of a left (side=-1) lifting surface; chord along -Z,
    thickness direction tilted by the cant angle (0 = horizontal wing)."""
    chord = z_le - z_te
    c = math.radians(cant)
    nx, ny = -side * math.sin(c), math.cos(c)

    def to3d(u, v):
        return cq.Vector(side * s + v * chord * nx, y_c + v * chord * ny, z_le - u * chord)

    return airfoil_wire(to3d, t)


def fin_section(y, z_le, z_te, t):
    chord = z_le - z_te

    def to3d(u, v):
        return cq.Vector(v * chord, y, z_le - u * chord)

    return airfoil_wire(to3d, t)


def loft(wires, ruled=True):
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, ruled))


def ring(z, yc, r, rot=45.0):
    # circle in a plane z = const; rotated so the loft seam lies on the
    # (+X,+Y) diagonal where it is least visible
    c = cq.Vector(0, yc, z)
    return cq.Wire.makeCircle(r, c, cq.Vector(0, 0, 1)).rotate(c, c + cq.Vector(0, 0, 1), rot)


def oval(z, yc, a, b):
    # ellipse, half-width a (X) and half-height b (Y), seam on the -X side
    c = cq.Vector(0, yc, z)
    return cq.Wire.makeEllipse(a, b, c, cq.Vector(0, 0, 1), cq.Vector(-1, 0, 0))


def tall_oval(z, yc, a, b):
    # ellipse with b >= a, seam on the top (+Y)
    c = cq.Vector(0, yc, z)
    return cq.Wire.makeEllipse(b, a, c, cq.Vector(0, 0, 1), cq.Vector(0, 1, 0))


# ---------------------------------------------------------------
# fuselage
barrel = (cq.Workplane("XY").workplane(offset=Z_TAIL)
          .transformed(rotate=(0, 0, 45)).circle(R_FUS).extrude(Z_NOSE - Z_TAIL))
nose = loft([tall_oval(*s) for s in NOSE_STATIONS], ruled=False)
tail = loft([ring(*s) for s in TAIL_STATIONS], ruled=False)
fuselage = barrel.union(nose).union(tail)

# belly fairing: smooth loft of ovals
fairing = loft([oval(*s) for s in FAIRING_STATIONS], ruled=False)
fuselage = fuselage.union(fairing)


# main wing (left half, then mirrored)
def le_z(s):
    if s <= KINK_S:
        return LE_ROOT_Z + (LE_KINK_Z - LE_ROOT_Z) * (s - S_SIDE) / (KINK_S - S_SIDE)
    return LE_KINK_Z - LE_SLOPE * (s - KINK_S)


def te_z(s):
    if s <= KINK_S:
        return TE_ROOT_Z + (TE_KINK_Z - TE_ROOT_Z) * s / KINK_S
    return TE_KINK_Z - TE_SLOPE * (s - KINK_S)


def wy(s):
    return WING_Y_ROOT + DIHEDRAL * (s - S_SIDE)


sec_root = wing_section(0.0, le_z(0.0), te_z(0.0), wy(0.0), T_ROOT)
sec_kink = wing_section(KINK_S, le_z(KINK_S), te_z(KINK_S), wy(KINK_S), T_KINK)
sec_out = wing_section(S_OUT, le_z(S_OUT), te_z(S_OUT), wy(S_OUT), T_OUT)
tip_secs = [wing_section(s, zl, zt, y, T_OUT, cant)
            for s, zl, zt, y, cant in TIP_SECTIONS]

wing_l = (loft([sec_root, sec_kink])
          .union(loft([sec_kink, sec_out]))
          .union(loft([sec_out] + tip_secs, ruled=False)))

# canoe-shaped fairing hanging below a surface: elliptic sections, top edge
# on local y = 0, running from z = 0 towards -Z
CANOE_SECTIONS = [  # (fraction of length, half-width, half-height) per unit size
    (0.0, 0.08, 0.12),
    (0.35, 0.45, 0.85),
    (0.72, 0.65, 1.3),
    (0.92, 0.5, 1.0),
    (1.0, 0.08, 0.14),
]


def canoe(length, size):
    wires = []
    for f, a, b in CANOE_SECTIONS:
        wires.append(cq.Wire.makeEllipse(a * size, b * size, cq.Vector(0, -0.8 * b * size, -f * length),
                                         cq.Vector(0, 0, 1), cq.Vector(1, 0, 0)))
    return loft(wires, ruled=False)


for s, z0, z1 in FLAP_TRACKS:
    p0 = (-s, wy(s), z0)
    ft = (canoe(z0 - z1, FT_SIZE).translate(p0)
          .rotate(p0, (p0[0] + 1, p0[1], p0[2]), -FT_DROOP))
    wing_l = wing_l.union(ft)


# engine (nacelle with open inlet + spinner + core nozzle + plug + pylon)
def engine():
    body = (cq.Workplane("XZ")
            .moveTo(0, NAC_REAR - 6.0)
            .lineTo(0.3, NAC_REAR - 6.0)
            .lineTo(2.3, NAC_REAR - 3.0)
            .lineTo(2.9, NAC_REAR - 3.0)
            .lineTo(3.3, NAC_REAR - 0.4)
            .lineTo(NAC_REAR_R, NAC_REAR)
            .spline([(NAC_R - 0.65, NAC_REAR + 6.0), (NAC_R, NAC_FRONT - 10.0),
                     (NAC_R - 0.15, NAC_FRONT - 4.5), (NAC_LIP_R, NAC_FRONT)],
                    includeCurrent=True)
            .lineTo(NAC_INLET_R, NAC_FRONT)
            .lineTo(NAC_INLET_R, NAC_FRONT - INLET_DEPTH)
            .lineTo(SPINNER_R, NAC_FRONT - INLET_DEPTH)
            .lineTo(0.0, NAC_FRONT - SPINNER_TIP_DEPTH)
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .rotate((0, 0, 0), (0, 0, 1), 45))
    # pylon: thin web from the nacelle top back under the wing
    wl = wy(ENG_X) - ENG_Y          # wing mean line above the engine axis
    pylon = (cq.Workplane("YZ")
             .polyline([(NAC_R - 1.0, NAC_FRONT - 9.0),
                        (wl + 0.2, le_z(ENG_X) - 1.0),
                        (wl + 0.2, te_z(ENG_X) + 5.0),
                        (wl - 1.0, te_z(ENG_X) + 5.0),
                        (3.0, NAC_REAR - 4.0),
                        (NAC_REAR_R - 0.8, NAC_REAR + 1.0)]).close()
             .extrude(0.75, both=True))
    return body.union(pylon)


eng = engine().translate((-ENG_X, ENG_Y, 0))
wing_l = wing_l.union(eng)
wing_r = wing_l.mirror("YZ")

# horizontal tail (straight panel + rounded tip)
hts = [wing_section(s, zl, zt, y, 0.10 if s == 0 else 0.09) for s, zl, zt, y in HT_SECTIONS]
ht_l = loft(hts[:2]).union(loft(hts[1:], ruled=False))
ht_r = ht_l.mirror("YZ")

# vertical fin (straight panel + rounded tip)
vts = [fin_section(y, zl, zt, VT_T_ROOT if i == 0 else VT_T_TIP) for i, (y, zl, zt) in enumerate(VT_SECTIONS)]
vt = loft(vts[:2]).union(loft(vts[1:], ruled=False))

result = (fuselage.union(wing_l).union(wing_r)
          .union(ht_l).union(ht_r).union(vt))

# antennas
for z, side, y0 in ANTENNAS:
    blade = (cq.Workplane("YZ")
             .polyline([(y0 - side * 0.5, z + ANT_L / 2), (y0 + side * ANT_H, z - ANT_L * 0.15),
                        (y0 + side * ANT_H, z - ANT_L / 2), (y0 - side * 0.5, z - ANT_L / 2)]).close()
             .extrude(ANT_T / 2, both=True))
    result = result.union(blade)

VIEW = {"azimuth": 45, "elevation": 26}
